import math
import cadquery as cq

# ---------------------------------------------------------------
# Mounting plate with rear slot bosses (bracket / carriage plate)
# X = width (left->right), Z = height (bottom->top), Y = thickness
# front face at Y = 0, rear features grow towards +Y
# ---------------------------------------------------------------
S = 0.4                      # mm per measured reference unit
W = 188.3 * S                # plate width  (~75 mm)
H = 95.0                     # plate height
T = 6.1                      # plate thickness
CH_OUT = 0.75                # chamfer on front outer perimeter
CH_WIN = 1.0                 # chamfer on front edges of the windows
CH_HOLE = 0.4                # chamfer on front edges of holes / slots

# rear bosses
LB_X0, LB_X1 = 27.8, 36.4    # left (centre) slot boss X range
LB_H = 11.8                  # left boss height above rear face
RB_X0 = 54.2                 # right block start X (to right edge)
RB_H = 7.7                   # right block height above rear face
RB_X0_LO = 50.0              # lower block starts inside the window (window trims it)
R_LBC = 4.0                  # lower-right block outer bottom corner
UP_Z = (0.0, 24.8)           # upper boss band, measured from top
LO_Z = (47.5, 63.4)          # lower boss band, measured from top
R_LB = 1.2                   # base fillet of centre bosses
R_RB = 3.0                   # base fillet of upper right block
R_COVE_T, R_COVE_B = 1.8, 1.5  # base coves of lower right block (top / bottom)
R_BC = 1.5                   # corner radius of bosses (plan view)
R_BACK = 0.8                 # rounding of the rear face edges of bosses

STRIP_X = (7.2, 16.8)        # raised rear strip along left hole column
STRIP_H = 1.1

# holes / slots
HOLE_D = 6.6
HOLES = [(11.8, 14.3), (11.9, 80.6)]          # (x, z from top)
TAP_D = 5.0
TAPS = [(34.7, 74.6), (58.6, 74.6)]
SLOT_W, SLOT_L = 4.4, 10.4
SLOT_X = [31.7, 68.8]
SLOT_Z = [18.0, 55.2]

# horizontal groove in the back of the upper right block
GROOVE_Z = 4.6               # from top
GROOVE_X = (56.8, 73.6)
GROOVE_W = 3.2
GROOVE_D = 3.0

R_WIN_RB = 4.0               # rear edge rounding of right window on blocks
R_WIN_LB = 1.5               # rear edge rounding of right window on bosses
R_WIN_TOP = 2.0              # rear edge rounding of right window top on the plate

# relief in the right window walls between the boss bands
RELIEF = 1.3
RELIEF_Z = (27.2, 46.0)      # relief extent, measured from top
RELIEF_Y0 = 0.2            # relief starts just behind the front chamfer


def Z(z_from_top):
    return H - z_from_top


def rounded_poly(wp, pts, radii):
    """closed polygon with per-vertex tangent fillet arcs (lines + arcs only)"""
    n = len(pts)
    segs = []
    for i in range(n):
        p = pts[i]
        a = pts[i - 1]
        b = pts[(i + 1) % n]
        r = radii[i]
        if r <= 0:
            segs.append((p, None, p))
            continue
        u1 = (a[0] - p[0], a[1] - p[1])
        u2 = (b[0] - p[0], b[1] - p[1])
        l1 = math.hypot(*u1)
        l2 = math.hypot(*u2)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (u2[0] / l2, u2[1] / l2)
        cosang = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
        th = math.acos(cosang) / 2.0
        d = r / math.tan(th)
        t1 = (p[0] + u1[0] * d, p[1] + u1[1] * d)
        t2 = (p[0] + u2[0] * d, p[1] + u2[1] * d)
        bx, by = u1[0] + u2[0], u1[1] + u2[1]
        bl = math.hypot(bx, by)
        bx, by = bx / bl, by / bl
        cdist = r / math.sin(th)
        c = (p[0] + bx * cdist, p[1] + by * cdist)
        m = (c[0] - bx * r, c[1] - by * r)
        segs.append((t1, m, t2))
    w = wp.moveTo(*segs[0][2])
    for i in range(1, n + 1):
        t1, m, t2 = segs[i % n]
        w = w.lineTo(*t1)
        if m is not None:
            w = w.threePointArc(m, t2)
    return w.close()


def prism(pts, radii, y0, y1):
    """extrude a rounded polygon (x,Z coords) from Y=y0 to Y=y1"""
    wp = cq.Workplane("XZ", origin=(0, y0, 0))
    return rounded_poly(wp, pts, radii).extrude(-(y1 - y0))


def rrect(x0, x1, z0, z1, r):
    return [(x0, z0), (x1, z0), (x1, z1), (x0, z1)], [r, r, r, r]


def box(x0, x1, z0, z1, y0, y1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------- plate outline ----------------
NOTCH_X = 67.8               # inner edge of the lower-right notch
STEP_Z = 83.7                # lower step edge (from top)
plate_pts = [
    (0.0, Z(0.0)),                      # top-left
    (W, Z(0.0)),                        # top-right
    (W, Z(61.5)),                       # right edge, start of notch slope
    (NOTCH_X, Z(69.0)),                 # notch inner (45 deg slope)
    (NOTCH_X, Z(STEP_Z)),               # notch bottom-right corner
    (30.0, Z(STEP_Z)),                  # step top
    (24.6, Z(H)),                       # step bottom
    (0.0, Z(H)),                        # bottom-left
]
plate_r = [4.8, 6.0, 3.5, 5.6, 8.0, 5.4, 5.6, 5.0]
plate = prism(plate_pts, plate_r, 0.0, T)

# ---------------- rear bosses ----------------
rear = None
for i, (zt, zb) in enumerate((UP_Z, LO_Z)):
    top = Z(zt) + (1.0 if i == 0 else 0.0)
    rt = 0.0 if i == 0 else R_BC
    lb = prism([(LB_X0, Z(zb)), (LB_X1, Z(zb)), (LB_X1, top), (LB_X0, top)],
               [R_BC, R_BC, rt, rt], T - 0.01, T + LB_H)
    rear = lb if rear is None else rear.union(lb)
# upper right block (runs into the rounded top-right corner)
rear = rear.union(prism([(RB_X0, Z(UP_Z[1])), (W + 1, Z(UP_Z[1])), (W + 1, Z(0) + 1),
                         (RB_X0, Z(0) + 1)], [R_BC, 0, 0, 0], T - 0.01, T + RB_H))

# clip rear features to plate outline
clip = prism(plate_pts, plate_r, T - 0.02, T + 30)
rear = rear.intersect(clip)
# lower right block: flush with the right edge, overhangs the notch slope
rear = rear.union(prism([(RB_X0_LO, Z(LO_Z[1])), (W, Z(LO_Z[1])), (W, Z(LO_Z[0])),
                         (RB_X0_LO, Z(LO_Z[0]))], [R_BC, R_LBC, 0, R_BC],
                        T - 0.01, T + RB_H))
body = plate.union(rear)

# concave fillets where the bosses meet the rear face
outline_w = rounded_poly(cq.Workplane("XZ", origin=(0, T, 0)), plate_pts, plate_r).wire().val()


def base_edges(x_lo, x_hi):
    sel = []
    for e in body.edges().vals():
        c = e.Center()
        if abs(c.y - T) > 1e-3:
            continue
        if not (x_lo <= c.x <= x_hi):
            continue
        m = e.positionAt(0.5)
        if cq.Vertex.makeVertex(m.x, m.y, m.z).distance(outline_w) < 0.3:
            continue
        sel.append(e)
    return sel


try:
    es = [e for e in base_edges(RB_X0 - 1.0, W + 1) if e.Center().z > Z(UP_Z[1]) - 1.0]
    body = body.newObject(es).fillet(R_RB)
except Exception as ex:
    print("right fillet failed", ex)


def cove(x0, x1, z_edge, direction, r):
    """concave fillet strip along X at the rear face (Y=T), on the +Z (1) or -Z (-1) side"""
    zc = z_edge + direction * r
    blk = box(x0, x1, min(z_edge, zc), max(z_edge, zc), T - 0.01, T + r)
    cyl = (cq.Workplane("YZ", origin=(x0 - 1, T + r, zc)).circle(r).extrude(x1 - x0 + 2))
    return blk.cut(cyl)


# manual coves for the lower right block (top and bottom edges)
coves = (cove(RB_X0_LO, W, Z(LO_Z[0]), 1, R_COVE_T)
         .union(cove(RB_X0_LO, W, Z(LO_Z[1]), -1, R_COVE_B))
         .intersect(prism(plate_pts, plate_r, T - 0.02, T + 30)))
body = body.union(coves)
try:
    es = base_edges(LB_X0 - 1.0, LB_X1 + 1.0)
    body = body.newObject(es).fillet(R_LB)
except Exception as ex:
    print("left fillet failed", ex)

strip = (cq.Workplane("XY")
         .polyline([(STRIP_X[0] - STRIP_H, T - 0.01), (STRIP_X[1] + STRIP_H, T - 0.01),
                    (STRIP_X[1], T + STRIP_H), (STRIP_X[0], T + STRIP_H)])
         .close().extrude(H))
body = body.union(strip)

# ---------------- windows ----------------
LWX0, LWX1 = 5.7, 25.5                  # left window walls (X)
LWZT, LWZB = 28.7, 66.4                 # left window walls (from top)
lw = [(LWX0, Z(LWZT)), (LWX1, Z(LWZT)), (LWX1, Z(LWZB)), (LWX0, Z(LWZB))]
lw_r = [5.5, 5.5, 5.5, 5.5]
RWX0, RWX1 = 37.7, 62.7                 # right window walls (X)
RWZT, RWZB = 15.0, 65.4                 # right window walls (from top)
rw = [(RWX0, Z(RWZT)), (RWX1, Z(RWZT)),
      (RWX1, Z(54.3)), (53.7, Z(RWZB)),  # chamfered lower-right corner
      (RWX0, Z(RWZB))]
rw_r = [5.5, 5.5, 3.0, 4.0, 5.5]
body = body.cut(prism(lw, lw_r, -1, T + 40)).cut(prism(rw, rw_r, -1, T + 40))


def window_edges(pts, radii, y, tol=0.05):
    w = rounded_poly(cq.Workplane("XZ", origin=(0, y, 0)), pts, radii).wire().val()
    sel = []
    for e in body.edges().vals():
        m = e.positionAt(0.5)
        if abs(m.y - y) > 1e-3:
            continue
        if abs(e.startPoint().y - y) > 1e-3 or abs(e.endPoint().y - y) > 1e-3:
            continue
        if cq.Vertex.makeVertex(m.x, m.y, m.z).distance(w) < tol:
            sel.append(e)
    return sel


# rounded rear edges of the right window on the blocks / bosses
for yy, rad in ((T + RB_H, R_WIN_RB), (T + LB_H, R_WIN_LB)):
    try:
        es = window_edges(rw, rw_r, yy)
        if es:
            body = body.newObject(es).fillet(rad)
    except Exception as ex:
        print("window fillet failed", yy, ex)

# rounded rear edge of the right window top, on the plate between boss and block
try:
    es = [e for e in window_edges(rw, rw_r, T) if e.positionAt(0.5).z > Z(RWZT) - 3.0]
    if es:
        nb = body.newObject(es).fillet(R_WIN_TOP)
        if nb.val().isValid():
            body = nb
except Exception as ex:
    print("window top fillet failed", ex)


def safe(old, new, tol=1e-3):
    """accept a filleted body only if valid and not growing"""
    try:
        v = new.val()
        if not v.isValid() or len(new.solids().vals()) != 1:
            return False
        a = old.val().BoundingBox()
        b = v.BoundingBox()
        if (b.xmin < a.xmin - tol or b.ymin < a.ymin - tol or b.zmin < a.zmin - tol or
                b.xmax > a.xmax + tol or b.ymax > a.ymax + tol or b.zmax > a.zmax + tol):
            return False
        return v.Volume() <= old.val().Volume() + 1e-6
    except Exception:
        return False


# soften the remaining (sharp) rear face edges of bosses and blocks
def sharp_back_edges(yy):
    out = []
    for e in body.edges().vals():
        if abs(e.startPoint().y - yy) > 1e-3 or abs(e.endPoint().y - yy) > 1e-3:
            continue
        m = e.positionAt(0.5)
        if cq.Vertex.makeVertex(m.x, T, m.z).distance(outline_w) < 0.3:
            continue
        out.append((round(m.x, 3), round(m.z, 3)))
    return out


for yy in (T + LB_H, T + RB_H):
    for (mx, mz) in sharp_back_edges(yy):
        cand = [e for e in body.edges().vals()
                if abs(e.startPoint().y - yy) < 1e-3 and abs(e.endPoint().y - yy) < 1e-3
                and abs(e.positionAt(0.5).x - mx) < 1e-3 and abs(e.positionAt(0.5).z - mz) < 1e-3]
        if not cand:
            continue
        try:
            nb = body.newObject(cand).fillet(R_BACK)
            if safe(body, nb):
                body = nb
        except Exception:
            pass


# ---------------- holes & slots ----------------
cutters = None
for (x, z) in HOLES:
    c = (cq.Workplane("XZ", origin=(x, -1, Z(z))).circle(HOLE_D / 2).extrude(-(T + 40)))
    cutters = c if cutters is None else cutters.union(c)
for (x, z) in TAPS:
    c = (cq.Workplane("XZ", origin=(x, -1, Z(z))).circle(TAP_D / 2).extrude(-(T + 40)))
    cutters = cutters.union(c)
for x in SLOT_X:
    for z in SLOT_Z:
        c = (cq.Workplane("XZ", origin=(x, -1, Z(z)))
             .slot2D(SLOT_L, SLOT_W, angle=90).extrude(-(T + 40)))
        cutters = cutters.union(c)
# groove on the back of the upper right block
gx = 0.5 * (GROOVE_X[0] + GROOVE_X[1])
gl = GROOVE_X[1] - GROOVE_X[0]
g = (cq.Workplane("XZ", origin=(gx, T + RB_H + 1, Z(GROOVE_Z)))
     .slot2D(gl, GROOVE_W, angle=0).extrude(1 + GROOVE_D))
cutters = cutters.union(g.translate((0, 0, 0)))
body = body.cut(cutters)

# front chamfer
outline_f = rounded_poly(cq.Workplane("XZ", origin=(0, 0, 0)), plate_pts, plate_r).wire().val()
lw_f = rounded_poly(cq.Workplane("XZ", origin=(0, 0, 0)), lw, lw_r).wire().val()
rw_f = rounded_poly(cq.Workplane("XZ", origin=(0, 0, 0)), rw, rw_r).wire().val()


def front_edges(kind):
    out = []
    for e in body.edges().vals():
        if abs(e.startPoint().y) > 1e-3 or abs(e.endPoint().y) > 1e-3:
            continue
        m = e.positionAt(0.5)
        v = cq.Vertex.makeVertex(m.x, 0, m.z)
        on_out = v.distance(outline_f) < 0.05
        on_win = v.distance(lw_f) < 0.05 or v.distance(rw_f) < 0.05
        k = "out" if on_out else ("win" if on_win else "hole")
        if k == kind:
            out.append(e)
    return out


for kind, ch in (("win", CH_WIN), ("out", CH_OUT), ("hole", CH_HOLE)):
    try:
        nb = body.newObject(front_edges(kind)).chamfer(ch)
        if safe(body, nb):
            body = nb
        else:
            print("chamfer rejected", kind)
    except Exception as ex:
        print("chamfer failed", kind, ex)

# relief of the right window side walls between the boss bands
# shallow circular (lens shaped) relief in both side walls of the right window
zt, zb = Z(RELIEF_Z[0]), Z(RELIEF_Z[1])
zm = 0.5 * (zt + zb)
half = 0.5 * (zt - zb)
r_lens = (half * half + RELIEF * RELIEF) / (2.0 * RELIEF)
for xw, sgn in ((RWX0, -1.0), (RWX1, 1.0)):
    xc = xw + sgn * (RELIEF - r_lens)
    disk = (cq.Workplane("XZ", origin=(xc, RELIEF_Y0, zm)).circle(r_lens)
            .extrude(-(T + 1 - RELIEF_Y0)))
    xa, xb = xw - sgn * 0.5, xw + sgn * (RELIEF + 1)
    lim = box(min(xa, xb), max(xa, xb), zb - 1, zt + 1, RELIEF_Y0 - 1, T + 2)
    body = body.cut(disk.intersect(lim))

result = body
